import math
import cadquery as cq

# ---------------------------------------------------------------
# Wheel with block-tread tyre, dished rim, 4-hole web and hub tube
# Axis of rotation = Z, part symmetric about the XY plane.
# All section coordinates are (radius, z) in mm.
# ---------------------------------------------------------------

# --- tyre -------------------------------------------------------
TIRE_R = 130.2          # outer radius on the crown (centre rows)
CROWN_R = 55.0          # crown radius of the centre tread band
Z_G1 = 18.7             # z of the two off-centre circumferential grooves
RIM_EDGE = (67.1, 33.3)  # rim edge / bead line (r, z)
SIDE_C = (93.65, 3.65)  # sidewall arc centre (tyre top = SIDE_C.z + SIDE_R)
SIDE_R = 39.8           # sidewall arc radius
SH_J_R = 102.0          # radius where the sidewall arc hands over to the shoulder
# shoulder curve (sidewall -> tread): flat conical land, then a tight
# round down the shoulder to the first circumferential groove
SH_PTS = [
    (110.0, 40.17),
    (119.44, 34.0),
    (123.36, 28.0),
    (125.52, 23.0),
]
SH_C = (90.37, 10.76)   # centre of the lower shoulder round (end tangent)
SH_R = 37.22

# --- rim / dish -------------------------------------------------
STEP_TOP = (51.0, 26.5)  # corner: sloped annulus -> steep dish wall
WEB_HALF_T = 2.2         # half thickness of the centre web
STEP_BOT = (43.0, WEB_HALF_T)  # corner: steep dish wall -> centre web
FIL_HUB = 3.0            # round where the hub tube meets the web
FIL_TOP = 6.0            # convex round at top of dish wall
FIL_BOT = 6.0            # concave round at bottom of dish wall

# --- hub tube ---------------------------------------------------
HUB_R = 20.35           # tube outer radius
HUB_HALF_L = 49.7       # tube half length
BORE_R = 15.2           # through bore radius
CBORE_R = 17.8          # counterbore radius at each end
CBORE_D = 12.5          # counterbore depth
CH = 0.8                # chamfer on bore mouth

# --- bolt holes -------------------------------------------------
HOLE_PCD_R = 34.0
HOLE_R = 4.0
N_HOLES = 4

# --- tread ------------------------------------------------------
N_PITCH = 20            # number of tread pitches round the tyre
GAP_ANG = 4.6           # angular width of the transverse gaps between blocks (deg)
GAP_D = 4.0             # depth of transverse gaps on the crown
GAP_END_R = 94.0        # radius on top of the sidewall where gaps run out
GAP_RAMP = 24.0         # length over which the gap floor ramps up to the surface
GAP_STEP = 5.0          # spacing of floor stations along the shoulder
GROOVE_W = 2.8          # circumferential groove width
GROOVE_D0 = 4.5         # depth of the centre groove
GROOVE_R1 = 124.3       # bottom radius of the two side grooves


# ---------------------------------------------------------------
def fillet_pts(p0, p1, p2, r):
    """Round corner p1 between segments p0-p1 and p1-p2.
    Returns (tangent point on p0-p1, arc mid point, tangent point on p1-p2)."""
    ux, uy = p0[0] - p1[0], p0[1] - p1[1]
    vx, vy = p2[0] - p1[0], p2[1] - p1[1]
    lu = math.hypot(ux, uy)
    lv = math.hypot(vx, vy)
    ux, uy, vx, vy = ux / lu, uy / lu, vx / lv, vy / lv
    ang = math.acos(max(-1.0, min(1.0, ux * vx + uy * vy)))
    t = r / math.tan(ang / 2.0)
    a = (p1[0] + ux * t, p1[1] + uy * t)
    b = (p1[0] + vx * t, p1[1] + vy * t)
    bx, by = ux + vx, uy + vy
    lb = math.hypot(bx, by)
    bx, by = bx / lb, by / lb
    d = r / math.sin(ang / 2.0)
    c = (p1[0] + bx * d, p1[1] + by * d)
    m = (c[0] - bx * r, c[1] - by * r)
    return a, m, b


def arc_mid(c, r, p, q):
    """Mid point of the short arc of circle (c, r) between p and q."""
    a1 = math.atan2(p[1] - c[1], p[0] - c[0])
    a2 = math.atan2(q[1] - c[1], q[0] - c[0])
    da = (a2 - a1 + math.pi) % (2 * math.pi) - math.pi
    am = a1 + da / 2.0
    return (c[0] + r * math.cos(am), c[1] + r * math.sin(am))


def mirror_pt(p):
    return (p[0], -p[1])


# crown arc (centre on the equator line)
CR_C = (TIRE_R - CROWN_R, 0.0)


def crown_r(z, off=0.0):
    return CR_C[0] + math.sqrt((CROWN_R - off) ** 2 - z * z)


P_CR = (crown_r(Z_G1), Z_G1)            # crown band edge
# hand-over point on the sidewall arc and its (clockwise) tangent
SH_J = (SH_J_R, SIDE_C[1] + math.sqrt(SIDE_R ** 2 - (SH_J_R - SIDE_C[0]) ** 2))
SH_J_T = ((SH_J[1] - SIDE_C[1]) / SIDE_R, -(SH_J[0] - SIDE_C[0]) / SIDE_R)
# end of shoulder curve at the first groove, tangent to the lower round
P_SH = (SH_C[0] + math.sqrt(SH_R ** 2 - (Z_G1 - SH_C[1]) ** 2), Z_G1)
P_SH_T = ((P_SH[1] - SH_C[1]) / SH_R, -(P_SH[0] - SH_C[0]) / SH_R)
SH_ALL = SH_PTS + [P_SH]


# ---------------------------------------------------------------
# upper half of the revolved section: list of segments
#   ("L", end) | ("A", mid, end) | ("S", [pts...], t0, t1)
# ---------------------------------------------------------------
def upper_half():
    segs = []
    start = (BORE_R, 0.0)
    segs.append(("L", (BORE_R, HUB_HALF_L - CBORE_D)))
    segs.append(("L", (CBORE_R, HUB_HALF_L - CBORE_D)))
    segs.append(("L", (CBORE_R, HUB_HALF_L - CH)))
    segs.append(("L", (CBORE_R + CH, HUB_HALF_L)))
    segs.append(("L", (HUB_R, HUB_HALF_L)))
    # hub tube -> web with a small round
    p_web = (HUB_R, WEB_HALF_T)
    a0, m0, b0 = fillet_pts((HUB_R, HUB_HALF_L), p_web, STEP_BOT, FIL_HUB)
    segs.append(("L", a0))
    segs.append(("A", m0, b0))
    # dish: web -> steep wall -> sloped annulus -> rim edge
    a1, m1, b1 = fillet_pts(p_web, STEP_BOT, STEP_TOP, FIL_BOT)
    a2, m2, b2 = fillet_pts(STEP_BOT, STEP_TOP, RIM_EDGE, FIL_TOP)
    segs.append(("L", a1))
    segs.append(("A", m1, b1))
    segs.append(("L", a2))
    segs.append(("A", m2, b2))
    segs.append(("L", RIM_EDGE))
    # tyre: sidewall arc, then one smooth shoulder curve to the groove
    segs.append(("A", arc_mid(SIDE_C, SIDE_R, RIM_EDGE, SH_J), SH_J))
    segs.append(("S", SH_ALL, SH_J_T, P_SH_T))
    segs.append(("L", P_CR))
    # crown arc to the equator
    p_eq = (TIRE_R, 0.0)
    segs.append(("A", arc_mid(CR_C, CROWN_R, P_CR, p_eq), p_eq))
    return start, segs


def seg_end(s):
    return s[1][-1] if s[0] == "S" else s[-1]


def mirror_segs(start, segs):
    """Lower half path from the equator back to start (mirror in z)."""
    pts = [start]
    for s in segs:
        pts.append(seg_end(s))
    out = []
    for i in range(len(segs) - 1, -1, -1):
        s = segs[i]
        tgt = mirror_pt(pts[i])
        if s[0] == "L":
            out.append(("L", tgt))
        elif s[0] == "A":
            out.append(("A", mirror_pt(s[1]), tgt))
        else:
            rp = [mirror_pt(p) for p in ([pts[i]] + s[1][:-1])][::-1]
            t0 = (-s[3][0], s[3][1])
            t1 = (-s[2][0], s[2][1])
            out.append(("S", rp, t0, t1))
    return out


def draw(wp, segs):
    for s in segs:
        if s[0] == "L":
            wp = wp.lineTo(*s[1])
        elif s[0] == "A":
            wp = wp.threePointArc(s[1], s[2])
        else:
            wp = wp.spline(s[1], tangents=[s[2], s[3]], includeCurrent=True)
    return wp


def build_section():
    start, up = upper_half()
    low = mirror_segs(start, up)
    wp = cq.Workplane("XZ").moveTo(*start)
    wp = draw(wp, up + low)
    return wp.close()


body = build_section().revolve(360.0, (0, 0, 0), (0, 1, 0))
# put the revolve seam in a tread gap at -X
body = body.rotate((0, 0, 0), (0, 0, 1), 180.0)

# --- circumferential grooves -----------------------------------
for zc, r_in in ((0.0, TIRE_R - GROOVE_D0), (Z_G1, GROOVE_R1), (-Z_G1, GROOVE_R1)):
    ring = (
        cq.Workplane("XZ")
        .moveTo(r_in, zc - GROOVE_W / 2)
        .lineTo(TIRE_R + 10, zc - GROOVE_W / 2)
        .lineTo(TIRE_R + 10, zc + GROOVE_W / 2)
        .lineTo(r_in, zc + GROOVE_W / 2)
        .close()
        .revolve(360.0, (0, 0, 0), (0, 1, 0))
    )
    body = body.cut(ring)


# --- transverse gaps between tread blocks ----------------------
def tyre_path():
    """sidewall + shoulder section curve as a wire in the XY plane (x=r, y=z)"""
    V = lambda p: cq.Vector(p[0], p[1], 0)
    return cq.Wire.assembleEdges([
        cq.Edge.makeThreePointArc(V(RIM_EDGE), V(arc_mid(SIDE_C, SIDE_R, RIM_EDGE, SH_J)), V(SH_J)),
        cq.Edge.makeSpline([V(SH_J)] + [V(p) for p in SH_ALL],
                           tangents=[V(SH_J_T), V(P_SH_T)]),
    ])


def gap_floor():
    """Floor points of a gap over the upper shoulder, from the run-out
    point on top of the sidewall down to the shoulder/crown junction.
    The floor follows the shoulder at depth GAP_D and ramps smoothly up
    to the surface over GAP_RAMP mm at the inner end."""
    e = tyre_path()
    total = e.Length()
    # locate the run-out parameter (radius == GAP_END_R; r grows along path)
    lo, hi = 0.0, 1.0
    for _ in range(60):
        mid = 0.5 * (lo + hi)
        if e.positionAt(mid).x < GAP_END_R:
            lo = mid
        else:
            hi = mid
    s0 = 0.5 * (lo + hi) * total
    span = total - s0
    n = max(4, int(math.ceil(span / GAP_STEP)))
    stations = [span * k / n for k in range(n + 1)]
    out = []
    for i, s in enumerate(stations):
        u = (s0 + s) / total
        p = e.positionAt(u)
        t = e.tangentAt(u)
        nx, nz = t.y, -t.x              # inward normal (towards body)
        x = min(s / GAP_RAMP, 1.0)
        d = GAP_D * (0.5 - 0.5 * math.cos(math.pi * x)) if i > 0 else -0.15
        out.append((p.x + nx * d, p.y + nz * d))
    out[-1] = (crown_r(Z_G1, GAP_D), Z_G1)
    return out


def gap_cutter():
    fl = gap_floor()                    # from run-out point down to Z_G1
    f_eq = (crown_r(0.0, GAP_D), 0.0)
    ztop = 60.0
    rout = TIRE_R + 15.0
    wp = cq.Workplane("XZ").moveTo(*f_eq)
    wp = wp.threePointArc(arc_mid(CR_C, CROWN_R - GAP_D, f_eq, fl[-1]), fl[-1])
    wp = wp.spline(fl[::-1][1:], includeCurrent=True)   # up the shoulder
    wp = wp.lineTo(fl[0][0], ztop)
    wp = wp.lineTo(rout, ztop)
    wp = wp.lineTo(rout, -ztop)
    wp = wp.lineTo(fl[0][0], -ztop)
    wp = wp.lineTo(*mirror_pt(fl[0]))
    wp = wp.spline([mirror_pt(p) for p in fl[1:]], includeCurrent=True)
    m_end = mirror_pt(fl[-1])
    wp = wp.threePointArc(arc_mid(CR_C, CROWN_R - GAP_D, m_end, f_eq), f_eq)
    wp = wp.close()
    # radial-walled gap of constant angular width, centred on +X
    cut = wp.revolve(GAP_ANG, (0, 0, 0), (0, 1, 0))
    return cut.rotate((0, 0, 0), (0, 0, 1), -GAP_ANG / 2.0)


gc = gap_cutter()
gaps = None
for k in range(N_PITCH):
    g = gc.rotate((0, 0, 0), (0, 0, 1), k * 360.0 / N_PITCH)
    gaps = g if gaps is None else gaps.union(g)
body = body.cut(gaps)

# --- bolt holes in the centre web -------------------------------
holes = None
for k in range(N_HOLES):
    a = math.radians(k * 360.0 / N_HOLES)
    h = (
        cq.Workplane("XY")
        .workplane(offset=-WEB_HALF_T - 5)
        .center(HOLE_PCD_R * math.cos(a), HOLE_PCD_R * math.sin(a))
        .circle(HOLE_R)
        .extrude(2 * WEB_HALF_T + 10)
    )
    holes = h if holes is None else holes.union(h)
body = body.cut(holes)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
